import math
import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_Sewing, BRepBuilderAPI_MakeSolid
from OCP.TopoDS import TopoDS
from OCP.ShapeFix import ShapeFix_Solid

# ---------------- driving dimensions (mm) ----------------
D_TIP = 20.3          # knurl tip (outside) diameter
H = 23.0              # overall height
N_TEETH = 22          # pyramids per row (diamond knurl, 2 x 22 crossing grooves)
TOOTH_H = 1.015       # knurl tooth height (tip to root)
ROW_PITCH = 2.02      # axial distance between pyramid rows
Z_ROW0 = 0.03         # height of a pyramid apex row
PHASE0 = 180.0 / N_TEETH  # angular position of the apexes of that row (deg)

TOP_FACE_D = 17.12    # flat top face diameter
TOP_CH_AX = 2.17      # axial length of the top chamfer cone (down to tip dia.)
BOT_FACE_D = 18.26    # flat bottom face outer diameter
BOT_CH_AX = 1.9       # axial length of the bottom chamfer cone (up to tip dia.)

BORE_D = 15.0         # blind bore from the underside
BORE_DEPTH = 9.55     # bore depth (top wall stays closed)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
R_T = D_TIP / 2.0
R_R = R_T - TOOTH_H
K_TWIST = math.pi / (N_TEETH * ROW_PITCH)     # groove twist rate, rad / mm
HELIX_PITCH = 2.0 * math.pi / K_TWIST
Z0, Z1 = -0.3, H + 0.3
PITCH_DEG = 360.0 / N_TEETH
ORIGIN = cq.Vector(0, 0, 0)
ZAXIS = cq.Vector(0, 0, 1)


def star_wire(phase):
    """Gear-like star: N triangular teeth (tip R_T, root R_R) at z = Z0."""
    pts = []
    for j in range(N_TEETH):
        th = 2.0 * math.pi * j / N_TEETH + phase
        pts.append(cq.Vector(R_T * math.cos(th), R_T * math.sin(th), Z0))
        th2 = th + math.pi / N_TEETH
        pts.append(cq.Vector(R_R * math.cos(th2), R_R * math.sin(th2), Z0))
    return cq.Wire.makePolygon(pts, close=True)


def twisted_star(sign):
    """Star prism swept with a helical twist = one hand of knurl grooves."""
    phase = math.radians(PHASE0) + sign * K_TWIST * (Z0 - Z_ROW0)
    prof = star_wire(phase)
    spine = cq.Wire.assembleEdges(
        [cq.Edge.makeLine(cq.Vector(0, 0, Z0), cq.Vector(0, 0, Z1))])
    aux = cq.Wire.makeHelix(HELIX_PITCH, Z1 - Z0, R_T * 0.5,
                            center=cq.Vector(0, 0, Z0), dir=ZAXIS,
                            lefthand=(sign < 0))
    return cq.Solid.sweep(prof, [], spine, True, False, aux)


# ---- revolved blank: chamfered cylinder with the blind bore ----
R_ENV = R_T + 0.6
r_top = TOP_FACE_D / 2.0
r_bot = BOT_FACE_D / 2.0
top_slope = (R_T - r_top) / TOP_CH_AX
bot_slope = (R_T - r_bot) / BOT_CH_AX
z_top_env = H - (R_ENV - r_top) / top_slope
z_bot_env = (R_ENV - r_bot) / bot_slope
r_bore = BORE_D / 2.0

blank = (cq.Workplane("XZ")
         .polyline([(r_bore, 0), (r_bot, 0), (R_ENV, z_bot_env),
                    (R_ENV, z_top_env), (r_top, H), (0, H),
                    (0, BORE_DEPTH), (r_bore, BORE_DEPTH)]).close()
         .revolve(360, (0, 0, 0), (0, 1, 0))).val()

grooves_r = twisted_star(+1)   # right-hand groove set
grooves_l = twisted_star(-1)   # left-hand groove set


def knurled_direct():
    return blank.intersect(grooves_r).intersect(grooves_l)


def knurled_by_sectors():
    """Diamond knurl = blank ∩ right-hand set ∩ left-hand set.
    Computed on one tooth-pitch sector (bounded by apex meridians) and
    polar-patterned N times; the sector copies are sewn together."""
    wedge = cq.Solid.makeCylinder(R_ENV + 5.0, H + 4.0, cq.Vector(0, 0, -2.0),
                                  ZAXIS, angleDegrees=PITCH_DEG)
    wedge = wedge.rotate(ORIGIN, ZAXIS, PHASE0)
    sector = blank.intersect(wedge).intersect(grooves_r).intersect(grooves_l)
    faces = [f for f in sector.Faces()
             if not (f.geomType() == "PLANE" and abs(f.normalAt().z) < 0.5)]
    sew = BRepBuilderAPI_Sewing(1e-4)
    for j in range(N_TEETH):
        for f in faces:
            sew.Add(f.rotate(ORIGIN, ZAXIS, PITCH_DEG * j).wrapped)
    sew.Perform()
    shell = TopoDS.Shell_s(sew.SewedShape())
    fix = ShapeFix_Solid(BRepBuilderAPI_MakeSolid(shell).Solid())
    fix.Perform()
    solid = cq.Solid(fix.Solid()).clean()
    expected = sector.Volume() * N_TEETH
    if not solid.isValid() or abs(solid.Volume() - expected) > 1e-3 * expected:
        raise ValueError("sector sewing failed")
    return solid


try:
    part = knurled_by_sectors()
except Exception:
    part = knurled_direct()

result = cq.Workplane("XY").add(part)
